import math
import cadquery as cq

# =====================================================================
#  Handset-like arm housing: small cylindrical head (top) with a
#  three-spoke grille, S-curved neck, large cylindrical foot (bottom).
#  X = width, Y = depth (front = -Y), Z = height.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R_TOP = 28.75          # head radius (axis along Y)
Z_TOP = 203.5          # head centre height
R_BOT = 38.0           # foot (barrel) max radius (axis along Y)
Z_BOT = 38.0           # foot centre height
BOT_DEPTH = 39.5       # foot depth (Y 0..BOT_DEPTH)
FOOT_R_FRONT = 34.5    # barrel radius at the front disc
FOOT_R_BACK = 36.3     # barrel radius at the back
CAP_R = 36.3           # back cap radius of the foot
CAP_T = 9.5            # back cap thickness
CAP_EDGE_R = 1.5       # rounding of the back cap edge
HEAD_RIM_R = 9.5       # rounding of the head front rim
HEAD_BACK_R = 2.0      # rounding of the head back disc edge
NECK_BACK_STEP = 1.2   # step between the head back disc and the neck
HEAD_IN = 0.3          # head cylinder sits this much inside the front silhouette
NECK_R = 14.0          # rounding of the neck long edges
DISC_R = 34.5          # flat front disc radius of the foot
HOLE_R = 6.0           # centre pocket radius (foot discs)
HOLE_D = 2.0           # centre pocket depth
HEAD_HOLE_R = 5.0      # centre pocket radius (head back disc)

GRILLE_R = 25.0        # grille recess radius
GRILLE_DEPTH = 13.0    # grille recess depth (along its axis)
GRILLE_ZC = 201.0      # grille centre height on the head face
GRILLE_TILT = 16.0     # grille axis tilt (deg, face looks up a little)
SPOKE_W = 4.0          # grille spoke width

BIG = 300.0
OS = 0.4               # oversize of the rounding trimmers


def circ_x(r, zc, z):
    return math.sqrt(r * r - (z - zc) ** 2)


# ---------------- front silhouette (XZ plane) ----------------
R_BOT_ENV = R_BOT + 0.2          # neck flank just covers the barrel
z1 = 200.0
z2 = 45.0
p1 = (circ_x(R_TOP, Z_TOP, z1), z1)
p2 = (circ_x(R_BOT_ENV, Z_BOT, z2), z2)
neck_side = [(27.4, 188.0), (25.7, 169.0), (24.8, 150.0), (25.0, 130.0),
             (26.3, 111.0), (28.2, 95.0), (31.2, 77.0), (35.3, 56.0)]
a1 = math.atan2(p1[1] - Z_TOP, p1[0])
t1 = (math.sin(a1), -math.cos(a1))
a2 = math.atan2(p2[1] - Z_BOT, p2[0])
t2 = (math.sin(a2), -math.cos(a2))
right_pts = [p1] + neck_side + [p2]
left_pts = [(-x, z) for (x, z) in reversed(right_pts)]

front_solid = (
    cq.Workplane("XZ", origin=(0, BIG / 2, 0))
    .moveTo(*p1)
    .spline(right_pts[1:], tangents=[t1, t2], includeCurrent=True)
    .threePointArc((0, Z_BOT - R_BOT_ENV), (-p2[0], p2[1]))
    .spline(left_pts[1:], tangents=[(-t2[0], -t2[1]), (-t1[0], -t1[1])],
            includeCurrent=True)
    .threePointArc((0, Z_TOP + R_TOP), p1)
    .close()
    .extrude(BIG)
)

# ---------------- side silhouette (YZ plane) ----------------
front_line = [(-11.0, 250.0), (-13.7, 232.25), (-17.5, 227.6), (-20.5, 220.0),
              (-25.0, 212.0), (-29.0, 204.0), (-31.6, 195.0), (-33.4, 180.0),
              (-34.0, 166.0), (-33.0, 157.0), (-30.0, 149.5), (-22.5, 129.0),
              (-15.5, 105.0), (-7.3, 74.2), (-1.9, 58.0), (0.0, 47.0),
              (1.0, 40.0)]
BACK_IN = BOT_DEPTH - 0.5
back_line = [(BACK_IN, 58.0), (34.0, 75.0), (28.5, 92.0), (22.0, 111.0),
             (14.0, 129.0), (4.5, 149.5), (0.8, 160.0), (0.0, 172.0)]

side_solid = (
    cq.Workplane("YZ", origin=(-BIG / 2, 0, 0))
    .moveTo(*front_line[0])
    .spline(front_line[1:], includeCurrent=True)
    .lineTo(1.0, -10.0)
    .lineTo(BACK_IN, -10.0)
    .lineTo(*back_line[0])
    .spline(back_line[1:], includeCurrent=True)
    .lineTo(0.0, 250.0)
    .close()
    .extrude(BIG)
)

envelope = front_solid.intersect(side_solid)
# neck overhang in front of the foot's flat front disc is removed
disc_cut = (cq.Workplane("XZ", origin=(0, 2.0, Z_BOT)).circle(DISC_R)
            .extrude(60))
envelope = envelope.cut(disc_cut)


# ---------------- rounding trimmers ----------------
def rounded_rect_wire(z, hw, yf, yb, rf, rb):
    """closed rounded-rectangle wire in the plane Z=z (front/back radii)"""
    cf = math.cos(math.radians(45)) * rf
    cb = math.cos(math.radians(45)) * rb
    wp = (cq.Workplane("XY").workplane(offset=z)
          .moveTo(-hw + rf, yf)
          .lineTo(hw - rf, yf)
          .threePointArc((hw - rf + cf, yf + rf - cf), (hw, yf + rf))
          .lineTo(hw, yb - rb)
          .threePointArc((hw - rb + cb, yb - rb + cb), (hw - rb, yb))
          .lineTo(-hw + rb, yb)
          .threePointArc((-hw + rb - cb, yb - rb + cb), (-hw, yb - rb))
          .lineTo(-hw, yf + rf)
          .threePointArc((-hw + rf - cf, yf + rf - cf), (-hw + rf, yf))
          .close())
    return wp.wires().val()


# exact envelope extents at a height z (sampled from the silhouette splines)
def _spline_edge(pts, tangents=None):
    vs = [cq.Vector(p[0], p[1], 0) for p in pts]
    tg = None if tangents is None else [cq.Vector(t[0], t[1], 0) for t in tangents]
    return cq.Edge.makeSpline(vs, tangents=tg, scale=True)


def _u_at(edge, z, n=600):
    best = None
    for i in range(n + 1):
        p = edge.positionAt(i / n)
        if best is None or abs(p.y - z) < abs(best.y - z):
            best = p
    return best.x


_e_side = _spline_edge(right_pts, [t1, t2])
_e_front = _spline_edge(front_line)
_e_back = _spline_edge(back_line)


def env_at(z):
    return _u_at(_e_side, z), _u_at(_e_front, z), _u_at(_e_back, z)


# neck: smooth loft through rounded-rectangle sections taken from the
# silhouettes; (z, front inset, side inset, front r, back r)
def neck_stations(nr):
    return [(NECK_Z0, 1.0, 0.0, 6.0, 6.0),
            (50.0, 0.0, -0.3, 9.0, 6.0),
            (70.0, 0.0, 0.0, 10.0, 5.0),
            (98.0, 0.0, 0.0, nr, 7.0),
            (126.0, 0.0, 0.0, nr, 10.0),
            (152.0, 0.0, 0.0, nr, 9.0),
            (176.0, 0.2, 0.0, 13.0, 2.5),
            (190.0, 0.4, 0.2, 12.0, 2.0),
            (Z_TOP, 0.5, 0.0, 11.0, 2.0)]


def make_neck(stations):
    wires = []
    for (z, fi, si, rf, rb) in stations:
        hw, yf, yb = env_at(z)
        if z <= NECK_Z0 + 0.1:
            # bottom section tucked inside the barrel foot
            hw, yf, yb = FOOT_R_FRONT - 0.3, 0.0, BOT_DEPTH - 1.0
        if z >= 175.0:
            # neck back sits just in front of the head's back disc
            yb = -NECK_BACK_STEP
        if z >= Z_TOP - 0.1:
            # top section tucked well inside the head
            hw = min(hw, circ_x(R_TOP - HEAD_IN - 0.3, Z_TOP, z))
            yb = -6.0
        wires.append(rounded_rect_wire(z, hw - si, yf + fi, yb, rf, rb))
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))


NECK_Z0 = 36.0

# head: slightly oversized head with a rounded front rim
head_front = [(y - OS, z) for (y, z) in front_line[:10]]
head_side = (
    cq.Workplane("YZ", origin=(-BIG / 2, 0, 0))
    .moveTo(*head_front[0])
    .spline(head_front[1:], includeCurrent=True)
    .lineTo(10.0, head_front[-1][1])
    .lineTo(10.0, 250.0)
    .close()
    .extrude(BIG)
)
head_cyl = (cq.Workplane("XZ", origin=(0, OS, Z_TOP)).circle(R_TOP - HEAD_IN)
            .extrude(80))
head_cyl = head_cyl.faces(">Y").edges().fillet(HEAD_BACK_R)
head_trim = head_cyl.intersect(head_side)
head_trim = (head_trim.edges(cq.selectors.BoxSelector((-50, -50, 100),
                                                       (50, -5, 260)))
             .fillet(HEAD_RIM_R))



def _ok(wp):
    try:
        sols = wp.solids().vals()
        return (len(sols) == 1 and sols[0].isValid() and wp.val().isValid()
                and sols[0].Volume() > 3e5)
    except Exception:
        return False


# head = envelope with a rounded front rim; neck = smooth loft
head_core = envelope.intersect(head_trim)
v_head = head_core.val().Volume()
core = None
for nr in (NECK_R, 12.0, 16.0):
    try:
        neck = make_neck(neck_stations(nr)).cut(disc_cut)
        v_neck = neck.val().Volume()
    except Exception:
        continue
    for tol in (None, 0.01, 0.05, 0.1):
        try:
            cand = neck.union(head_core, tol=tol)
        except Exception:
            continue
        if _ok(cand):
            v = cand.solids().vals()[0].Volume()
            if v_neck + 0.3 * v_head < v < v_neck + v_head + 1.0:
                core = cand
                break
    if core is not None:
        break
if core is None:
    core = envelope

# ---------------- foot: Y-axis cylinder + back cap ----------------
# barrel: bulges from the front disc to R_BOT and eases off towards the back
foot = (cq.Workplane("YZ", origin=(0, 0, Z_BOT))
        .moveTo(0, 0)
        .lineTo(0, FOOT_R_FRONT)
        .threePointArc((BOT_DEPTH * 0.5, R_BOT), (BOT_DEPTH, FOOT_R_BACK))
        .lineTo(BOT_DEPTH, 0)
        .close()
        .revolve(360.0, (0, 0, 0), (1, 0, 0)))
cap = (cq.Workplane("XZ", origin=(0, BOT_DEPTH + CAP_T, Z_BOT)).circle(CAP_R)
       .extrude(CAP_T + 1.0))
cap = cap.faces(">Y").edges().fillet(CAP_EDGE_R)

body = core.union(foot).union(cap)

# ---------------- grille in the head's front face ----------------
gy = -29.9                                    # face Y at the grille centre
g_t = math.radians(GRILLE_TILT)
n_in = cq.Vector(0, math.cos(g_t), -math.sin(g_t))   # into the part
g_c = cq.Vector(0, gy, GRILLE_ZC)
g_org = g_c - n_in * 15.0
g_plane = cq.Plane(origin=g_org, xDir=(1, 0, 0), normal=n_in)
g_len = 15.0 + GRILLE_DEPTH
pocket = cq.Workplane(g_plane).circle(GRILLE_R).extrude(g_len)


def spoke_pts(ang_deg, length, width):
    a = math.radians(ang_deg)
    ux, uy = math.cos(a), math.sin(a)
    vx, vy = -uy, ux
    hw = width / 2
    return [(vx * hw, vy * hw), (ux * length + vx * hw, uy * length + vy * hw),
            (ux * length - vx * hw, uy * length - vy * hw), (-vx * hw, -vy * hw)]


spokes = cq.Workplane(g_plane).circle(SPOKE_W * 0.8).extrude(g_len)
for ang in (90.0, -30.0, -150.0):   # local +y points down the face
    sp = (cq.Workplane(g_plane).polyline(spoke_pts(ang, GRILLE_R + 2.0, SPOKE_W))
          .close().extrude(g_len))
    spokes = spokes.union(sp)
body = body.cut(pocket.cut(spokes))


# ---------------- centre pockets of the three discs ----------------
foot_hole = (cq.Workplane("XZ", origin=(0, 1.0, Z_BOT)).circle(HOLE_R)
             .extrude(1.0 + HOLE_D))
cap_hole = (cq.Workplane("XZ", origin=(0, BOT_DEPTH + CAP_T - HOLE_D, Z_BOT))
            .circle(HOLE_R).extrude(-(HOLE_D + 1.0)))
head_hole = (cq.Workplane("XZ", origin=(0, -HOLE_D, Z_TOP))
             .circle(HEAD_HOLE_R).extrude(-(HOLE_D + 1.0)))
body = body.cut(foot_hole).cut(cap_hole).cut(head_hole)

# ---------------- small tab on top of the head ----------------
TAB_R = 4.0
TAB_Y0, TAB_Y1 = -9.8, -6.5
top_tab = (cq.Workplane("XZ", origin=(0, TAB_Y1, Z_TOP + R_TOP - 0.5))
           .circle(TAB_R).extrude(TAB_Y1 - TAB_Y0))
body = body.union(top_tab)

# ---------------- boss on the back of the neck below the head ----------------
BB_W, BB_Z0, BB_Z1, BB_Y1 = 14.0, 158.2, 168.8, 12.3
back_boss = (cq.Workplane("XY").box(BB_W, BB_Y1 + 6.0, BB_Z1 - BB_Z0,
                                    centered=(True, False, False))
             .translate((0, -6.0, BB_Z0))
             .edges(">Y").fillet(3.0))
body = body.union(back_boss)

# ---------------- connector hood with two pins on the +X side ----------------
CB_Y0, CB_Y1, CB_Z0, CB_Z1, CB_X1 = 9.0, 31.7, 66.3, 78.8, 39.5
CB_X0 = 26.0
conn_boss = (cq.Workplane("YZ", origin=(CB_X0, 0, 0))
             .center((CB_Y0 + CB_Y1) / 2, (CB_Z0 + CB_Z1) / 2)
             .rect(CB_Y1 - CB_Y0, CB_Z1 - CB_Z0).extrude(CB_X1 - CB_X0)
             .edges("|X and >Z").fillet(7.0))
# outer face curved like a quarter round (axis along Y)
hood_round = (cq.Workplane("XZ", origin=(CB_X0, CB_Y1 + 1.0, CB_Z0))
              .circle(CB_X1 - CB_X0).extrude(CB_Y1 - CB_Y0 + 2.0))
conn_boss = conn_boss.intersect(hood_round)
body = body.union(conn_boss)
for py in (14.8, 25.4):
    pin = (cq.Workplane("XY", origin=(35.0, py, 60.0)).circle(2.2)
           .extrude(CB_Z0 - 60.0 + 1.0))
    body = body.union(pin)

# ---------------- hinge lugs with clip pins on the -X side of the foot -------
LUG_T = 5.5
LUG_YS = (21.5, 39.8)                 # lug mid-planes (Y)
for ly in LUG_YS:
    lug = (cq.Workplane("XZ", origin=(0, ly + LUG_T / 2, 0))
           .moveTo(-30.0, 53.0)
           .lineTo(-42.0, 50.0)
           .threePointArc((-54.0, 36.5), (-42.0, 21.0))
           .lineTo(-30.0, 17.0)
           .close()
           .extrude(LUG_T))
    body = body.union(lug)
    # clip block under the lug, pin with a rounded head below it
    clip = (cq.Workplane("XY").box(7.0, LUG_T, 6.0)
            .translate((-34.5, ly, 17.0))
            .edges("<Z").fillet(1.5))
    pin = (cq.Workplane("XY", origin=(-34.5, ly, 7.5)).circle(1.8)
           .extrude(7.0))
    pin_head = (cq.Workplane("XY", origin=(-34.5, ly, 6.0)).circle(2.4)
                .extrude(2.0).edges("<Z").fillet(0.8))
    body = body.union(clip).union(pin).union(pin_head)
dome = (cq.Workplane("XY", origin=(-39.0, LUG_YS[1] + LUG_T / 2 - 1.0, 24.0))
        .sphere(4.0))
dome = dome.intersect(cq.Workplane("XY").box(20, 20, 20)
                      .translate((-39.0, LUG_YS[1] + LUG_T / 2 + 10.0 - 1.0, 24.0)))
body = body.union(dome)

# ---------------- raised handset emblem below the grille ----------------
EM_Y0, EM_Y1 = -31.5, -34.9          # emblem extrusion (from inside to proud)
em_path = [(-11.8, 161.5), (-6.0, 167.2), (6.0, 167.2), (11.8, 161.5)]
em_plane = cq.Plane(origin=(0, EM_Y0, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
emblem = (cq.Workplane(em_plane).polyline(em_path).offset2D(1.3)
          .extrude(EM_Y0 - EM_Y1))
for ex in (-11.8, 11.8):
    pad = cq.Workplane(em_plane).center(ex, 161.5).circle(2.6).extrude(EM_Y0 - EM_Y1)
    emblem = emblem.union(pad)
    emblem = emblem.cut(cq.Workplane(em_plane).center(ex, 161.5).circle(1.0)
                        .extrude(EM_Y0 - EM_Y1 + 1.0))
for ex in (-1.6, 1.6):
    emblem = emblem.cut(cq.Workplane(em_plane).center(ex, 167.2).circle(0.6)
                        .extrude(EM_Y0 - EM_Y1 + 1.0))
body = body.union(emblem)

result = body
